import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 150.0            # overall length (X)
W = 98.0             # overall width (Y)
T = 4.8              # overall height of plate (rim / ring top)
FLOOR = 0.9          # floor thickness inside the tray
WALL = 2.8           # perimeter wall thickness
BOT_CHAMFER = 2.4    # chamfer on the bottom outer edge

R_LEFT = 7.0         # corner radius at the -X corners
R_BR = 17.5          # corner radius at the +X/-Y corner
CH_X = 28.5          # corner chamfer run along the +Y edge (+X/+Y corner)
CH_Y = 16.6          # corner chamfer run along the +X edge
R_CH = 5.0           # small round at both ends of the corner chamfer

HOLE_R = 35.7        # central through hole radius
FLARE_W = 7.0        # radial run of the flared hole wall (top edge -> underside)
RING_R = 45.8        # raised ring outer radius
BRIDGE_X0 = -14.8    # ring-to-wall bridges at +/-Y span x = BRIDGE_X0..BRIDGE_X1
BRIDGE_X1 = 13.1

RIB_W = 3.0          # rib width
RIB_H = 2.0          # rib height above floor

SLOT_W = 1.6         # width of the small slots in the rim
SLOT_L_BR = 12.3     # length of the slots in the +/-Y bridges
SLOT_L_LF = 13.0     # length of the slots in the -X wall blocks
SLOT_L_RT = 12.5     # length of the slot in the +X wall block
SLOT_IN = 1.4        # slot centre-line distance from the outer edge
SLOT_D = 2.4         # slot depth
BRIDGE_SLOT_X = -6.0 # slot centre (x) in the +/-Y bridges

LBLK_Y = 21.0        # -X wall blocks at y = +/-LBLK_Y
LBLK_L = 18.7        # their length along Y
LBLK_T = 2.2         # how far they stand in from the wall
RBLK_L = 18.8        # +X wall block
RBLK_Y = -0.6        # +X wall block / slot centre (y)
RBLK_T = 2.3
BLK_R = 0.0          # optional round on the inner corners of the wall blocks (0 = sharp)

BOSS_X = L / 2 - 16.1   # boss centre X
BOSS_Y = 23.5           # boss centre +/- Y
BASE_S = 12.6           # boss base (rounded square) size
BASE_R = 5.0
POST_S = 6.4            # boss post size
POST_R = 1.5
POST_TOP = T + 5.6      # post top height
POST_EDGE = 0.4         # small round on the post top edge
BOSS_HOLE_D = 2.5
BOSS_CSK_D = 4.9

Z0 = FLOOR * 0.5        # start height of features grown from the floor
OVL = 0.5               # overlap of features into the walls


# ---------------- helpers ----------------
def rounded_poly(pts, radii):
    """Closed wire through pts (XY, CCW) with a tangent arc of radius r at every vertex."""
    n = len(pts)
    segs = []
    for i in range(n):
        p0 = pts[i - 1]
        p1 = pts[i]
        p2 = pts[(i + 1) % n]
        r = radii[i]
        v1 = (p0[0] - p1[0], p0[1] - p1[1])
        v2 = (p2[0] - p1[0], p2[1] - p1[1])
        l1 = math.hypot(*v1)
        l2 = math.hypot(*v2)
        u1 = (v1[0] / l1, v1[1] / l1)
        u2 = (v2[0] / l2, v2[1] / l2)
        cosang = u1[0] * u2[0] + u1[1] * u2[1]
        ang = math.acos(max(-1.0, min(1.0, cosang)))
        d = r / math.tan(ang / 2)
        a = (p1[0] + u1[0] * d, p1[1] + u1[1] * d)
        b = (p1[0] + u2[0] * d, p1[1] + u2[1] * d)
        bis = (u1[0] + u2[0], u1[1] + u2[1])
        bl = math.hypot(*bis)
        bis = (bis[0] / bl, bis[1] / bl)
        h = r / math.sin(ang / 2)
        c = (p1[0] + bis[0] * h, p1[1] + bis[1] * h)
        m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
        segs.append((a, m, b))
    wp = cq.Workplane("XY").moveTo(*segs[0][2])
    for i in range(1, n + 1):
        a, m, b = segs[i % n]
        wp = wp.lineTo(*a)
        wp = wp.threePointArc(m, b)
    return wp.close()


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(abs(x1 - x0), abs(y1 - y0)).extrude(z1 - z0))


hx, hy = L / 2, W / 2
OUTLINE = [(-hx, -hy), (hx, -hy), (hx, hy - CH_Y), (hx - CH_X, hy), (-hx, hy)]
RADII = [R_LEFT, R_BR, R_CH, R_CH, R_LEFT]

# ---------------- main body: shallow tray ----------------
body = rounded_poly(OUTLINE, RADII).extrude(T)
body = body.faces("<Z").edges().chamfer(BOT_CHAMFER)

pocket = (rounded_poly(OUTLINE, RADII).offset2D(-WALL)
          .extrude(T).translate((0, 0, FLOOR)))
body = body.cut(pocket)

# raised ring around the central opening (flush with the rim)
ring = cq.Workplane("XY").workplane(offset=Z0).circle(RING_R).extrude(T - Z0)
body = body.union(ring)

# solid bridges joining the ring to the +/-Y walls
for s in (1, -1):
    y_in = s * (RING_R - 6.0)
    y_out = s * (hy - WALL + OVL)
    body = body.union(box(BRIDGE_X0, BRIDGE_X1, y_in, y_out, Z0, T))

# thickened wall blocks (-X wall: two, +X wall: one)
for s in (1, -1):
    blk = box(-hx + WALL - OVL, -hx + WALL + LBLK_T,
              s * LBLK_Y - LBLK_L / 2, s * LBLK_Y + LBLK_L / 2, Z0, T)
    if BLK_R > 0:
        blk = blk.edges("|Z").edges(">X").fillet(BLK_R)
    body = body.union(blk)
blk = box(hx - WALL - RBLK_T, hx - WALL + OVL,
          RBLK_Y - RBLK_L / 2, RBLK_Y + RBLK_L / 2, Z0, T)
if BLK_R > 0:
    blk = blk.edges("|Z").edges("<X").fillet(BLK_R)
body = body.union(blk)

# low ribs along the X axis
body = body.union(box(-hx + WALL - OVL, -RING_R + 1.0,
                      -RIB_W / 2, RIB_W / 2, Z0, FLOOR + RIB_H))
body = body.union(box(RING_R - 1.0, hx - WALL - RBLK_T + OVL,
                      -RIB_W / 2, RIB_W / 2, Z0, FLOOR + RIB_H))

# screw bosses: rounded-square base + rounded-square post with countersunk pilot hole
for s in (1, -1):
    cx, cy = BOSS_X, s * BOSS_Y
    base = (cq.Workplane("XY").workplane(offset=Z0).center(cx, cy)
            .rect(BASE_S, BASE_S).extrude(T - Z0)
            .edges("|Z").fillet(BASE_R))
    post = (cq.Workplane("XY").workplane(offset=Z0).center(cx, cy)
            .rect(POST_S, POST_S).extrude(POST_TOP - Z0)
            .edges("|Z").fillet(POST_R)
            .faces(">Z").edges().fillet(POST_EDGE))
    body = body.union(base).union(post)
    pilot = (cq.Workplane("XY").workplane(offset=POST_TOP - 6.0)
             .center(cx, cy).circle(BOSS_HOLE_D / 2).extrude(7.0))
    body = body.cut(pilot)
    ch = (BOSS_CSK_D - BOSS_HOLE_D) / 2
    csk = cq.Solid.makeCone(BOSS_HOLE_D / 2, BOSS_CSK_D / 2 + 0.05, ch + 0.05,
                            pnt=cq.Vector(cx, cy, POST_TOP - ch))
    body = body.cut(cq.Workplane("XY").add(csk))

# central opening: sharp top edge, the wall sweeps out in one circular arc that
# runs tangent into the underside (revolved profile)
FL_R = (FLARE_W ** 2 + T ** 2) / (2 * T)           # arc radius
FL_C = HOLE_R + FLARE_W                             # arc centre (radial), centre z = FL_R
_a0 = math.atan2(T - FL_R, HOLE_R - FL_C)
_a1 = -math.pi / 2
_am = (_a0 + _a1) / 2
_mid = (FL_C + FL_R * math.cos(_am), FL_R + FL_R * math.sin(_am))
opening = (cq.Workplane("XZ")
           .moveTo(0, -1)
           .lineTo(FL_C, -1)
           .lineTo(FL_C, 0)
           .threePointArc(_mid, (HOLE_R, T))
           .lineTo(HOLE_R, T + 1)
           .lineTo(0, T + 1)
           .close()
           .revolve(360, (0, 0, 0), (0, 1, 0)))
body = body.cut(opening)

# small slots in the rim top
slot_specs = [
    (BRIDGE_SLOT_X, hy - SLOT_IN, 0.0, SLOT_L_BR),
    (BRIDGE_SLOT_X, -hy + SLOT_IN, 0.0, SLOT_L_BR),
    (-hx + SLOT_IN, LBLK_Y, 90.0, SLOT_L_LF),
    (-hx + SLOT_IN, -LBLK_Y, 90.0, SLOT_L_LF),
    (hx - SLOT_IN, RBLK_Y, 90.0, SLOT_L_RT),
]
for (sx, sy, ang, sl_len) in slot_specs:
    sl = (cq.Workplane("XY").workplane(offset=T - SLOT_D)
          .center(sx, sy).slot2D(sl_len, SLOT_W, ang).extrude(SLOT_D + 1))
    body = body.cut(sl)

result = body
